import math
import cadquery as cq

# =====================================================================
#  Hexagonal coaster / tile with a raised eight-ray "sun" emblem.
#  The emblem is a raised plateau whose outline is a closed chain of
#  spline edges (flame-like rays), with a narrow annular groove cut
#  around a raised centre disk.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
HEX_R = 50.0             # hexagon circumradius (corners on +/-X)
PLATE_T = 7.6            # plate thickness
SUN_H = 3.8              # height of the raised emblem above the plate
SUN_CX, SUN_CY = 0.35, 0.5   # emblem centre (slightly off the hex centre)
SUN_SCALE = HEX_R / 50.0     # emblem outline is defined for HEX_R = 50
RING_R_OUT = 16.05 * SUN_SCALE   # outer radius of the annular groove
RING_R_IN = 14.65 * SUN_SCALE    # radius of the raised centre disk
RING_DX, RING_DY = -0.18, 0.22   # groove centre offset from the emblem centre
RING_SEAM_ANGLE = 225.0          # where the cylindrical faces start (deg)

# Emblem outline: chain of spline segments (x, y relative to the emblem
# centre, for HEX_R = 50).  Consecutive segments share their end points;
# those shared points are the sharp corners of the outline (ray tips,
# barbs and valley kinks).  Rays are listed counter-clockwise starting at
# the tip of the ray pointing up (+Y).
SUN_OUTLINE = [
    [(5.57, 38.38), (4.44, 37.53), (2.68, 36.35), (0.60, 34.91), (-2.21, 33.00), (-4.14, 31.44), (-5.71, 29.66), (-7.32, 27.65), (-7.65, 26.59), (-7.43, 25.86)],
    [(-7.43, 25.86), (-5.35, 24.12), (-4.12, 20.74), (-5.82, 17.41), (-8.13, 16.71)],
    [(-8.13, 16.71), (-8.87, 17.74), (-10.05, 19.75), (-12.05, 21.56), (-13.10, 21.85), (-14.15, 21.75), (-17.32, 20.86), (-20.46, 23.40), (-21.30, 25.83), (-21.77, 27.66), (-22.81, 30.55)],
    [(-22.81, 30.55), (-23.27, 28.44), (-23.69, 25.07), (-24.35, 21.96), (-24.92, 18.05), (-24.74, 15.27), (-24.42, 13.34)],
    [(-24.42, 13.34), (-21.67, 13.49), (-17.71, 12.04), (-16.48, 8.13), (-18.03, 5.95)],
    [(-18.03, 5.95), (-19.06, 5.97), (-21.38, 6.28), (-23.08, 6.45), (-24.07, 6.30), (-25.02, 5.47), (-25.94, 3.53), (-27.24, 2.40), (-31.14, 2.38), (-33.97, 3.47), (-36.50, 4.60), (-37.80, 5.29)],
    [(-37.80, 5.29), (-36.72, 3.58), (-34.69, 0.09), (-32.96, -2.82), (-30.67, -5.65), (-29.21, -6.96), (-26.32, -7.83), (-24.61, -7.23), (-23.36, -5.85), (-21.74, -3.94), (-19.95, -3.62), (-19.04, -4.03), (-17.73, -5.59), (-17.10, -7.51), (-17.60, -8.09), (-19.31, -9.13), (-21.39, -11.80), (-21.75, -13.01), (-21.72, -14.61), (-21.34, -16.65), (-21.00, -17.63)],
    [(-21.00, -17.63), (-22.86, -19.16), (-25.73, -20.34), (-30.98, -22.08)],
    [(-30.98, -22.08), (-21.69, -23.75), (-16.21, -23.55), (-12.49, -22.46)],
    [(-12.49, -22.46), (-12.64, -19.03), (-12.57, -17.83), (-12.16, -16.67), (-11.53, -16.10), (-10.38, -15.84), (-8.06, -16.27), (-6.45, -17.53), (-6.51, -19.37), (-6.89, -20.86), (-6.85, -21.82), (-6.48, -22.75), (-5.44, -24.24), (-3.38, -26.86), (-2.15, -29.10), (-3.35, -32.98), (-4.46, -34.94), (-5.65, -36.82), (-6.19, -38.18)],
    [(-6.19, -38.18), (1.68, -33.21), (5.48, -29.32), (7.54, -26.09)],
    [(7.54, -26.09), (5.66, -24.35), (4.24, -22.93), (3.62, -20.53), (4.16, -18.72), (5.11, -17.70), (7.09, -16.77), (8.64, -16.40)],
    [(8.64, -16.40), (9.48, -17.51), (10.67, -19.49), (11.59, -20.53), (12.61, -21.22), (13.74, -21.37), (15.82, -20.66), (18.10, -20.34), (19.75, -21.22), (20.68, -23.28), (21.83, -27.18), (23.06, -30.53)],
    [(23.06, -30.53), (23.05, -28.80), (23.52, -26.11), (24.37, -21.31), (25.27, -16.68), (24.69, -14.06), (24.01, -12.30)],
    [(24.01, -12.30), (21.39, -12.66), (19.49, -12.49), (17.35, -10.98), (16.46, -9.08), (16.55, -7.35), (17.39, -5.64), (18.36, -4.55)],
    [(18.36, -4.55), (19.33, -4.76), (21.22, -5.25), (23.75, -5.20), (26.47, -2.08), (27.66, -0.90), (29.33, -0.48), (31.73, -1.03), (35.72, -3.15), (38.05, -4.09)],
    [(38.05, -4.09), (37.23, -3.18), (36.20, -1.59), (34.21, 1.07), (33.08, 3.24), (32.01, 4.78), (30.41, 6.52), (28.32, 8.35), (26.31, 8.81), (25.07, 8.45), (23.85, 7.37), (22.62, 5.97), (20.42, 4.60), (18.50, 5.16), (16.92, 7.42), (16.39, 8.68)],
    [(16.39, 8.68), (16.94, 9.27), (17.99, 10.09), (19.98, 12.15), (20.33, 15.01), (20.89, 18.06), (22.62, 20.15), (25.09, 21.17), (26.82, 21.83), (28.50, 22.68), (30.09, 23.48)],
    [(30.09, 23.48), (29.02, 23.83), (27.53, 24.18), (25.31, 24.78), (22.56, 25.15), (20.05, 25.41), (17.26, 25.22), (14.92, 24.85), (13.22, 24.27), (12.54, 23.49), (12.34, 22.49), (12.39, 20.88), (12.18, 18.12), (11.62, 17.17), (10.87, 16.75), (9.86, 16.76), (8.49, 16.99), (6.84, 17.09), (5.90, 17.63)],
    [(5.90, 17.63), (5.77, 18.34), (6.10, 19.63), (6.72, 21.28), (6.57, 22.96), (4.50, 25.66), (2.61, 27.67), (2.00, 30.70), (2.98, 33.14), (4.30, 35.44), (5.06, 37.27), (5.57, 38.38)],
]


def sun_wire():
    edges = []
    for seg in SUN_OUTLINE:
        pts = [cq.Vector(SUN_CX + SUN_SCALE * x, SUN_CY + SUN_SCALE * y, 0.0)
               for x, y in seg]
        edges.append(cq.Edge.makeSpline(pts))
    return cq.Wire.assembleEdges(edges)


# ---------------- hexagonal plate ----------------
plate = cq.Workplane("XY").polygon(6, 2 * HEX_R).extrude(PLATE_T)

# ---------------- raised emblem ----------------
sun_face = cq.Face.makeFromWires(sun_wire())
sun = (
    cq.Workplane("XY")
    .add(cq.Solid.extrudeLinear(sun_face, cq.Vector(0, 0, SUN_H)))
    .translate((0, 0, PLATE_T))
)

# annular groove between the emblem body and the centre disk
ring_plane = cq.Plane(
    origin=(SUN_CX + RING_DX * SUN_SCALE, SUN_CY + RING_DY * SUN_SCALE, PLATE_T),
    xDir=(math.cos(math.radians(RING_SEAM_ANGLE)),
          math.sin(math.radians(RING_SEAM_ANGLE)), 0.0),
    normal=(0, 0, 1),
)
groove = (
    cq.Workplane(ring_plane)
    .circle(RING_R_OUT)
    .circle(RING_R_IN)
    .extrude(SUN_H)
)

result = plate.union(sun).cut(groove)

VIEW = {"azimuth": 45, "elevation": 26}
